import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0            # outer diameter of the wheel rim
H = 30.0             # overall height
R = D / 2.0
BORE_R = 37.5        # bottom bore radius (open underneath)
WEB_Z = 20.0         # height of the bore ceiling = underside of spokes
OPEN_R = BORE_R      # outer radius of the three window cut-outs (flush with bore)
SPOKE_W = 10.0       # spoke width
N_SPOKES = 3
SPOKE0 = 90.0        # angle of first spoke (deg)
CORNER_R = 5.0       # plan-view radius of the window outer corners
APEX_R = 2.0         # plan-view radius at the window apex (hidden in hub)
EDGE_FILLET = 4.95   # round-over of the window top edges (spokes ~ fully round)
HUB_D = 15.0         # centre hub diameter (full height)

VIEW = {"azimuth": 45, "elevation": 26}

V = cq.Vector


def window_solid(theta_deg, z0, z1):
    """Prism of one window (plan: sector between two spokes with rounded
    corners), centred on angle theta_deg, spanning z0..z1."""
    hw = SPOKE_W / 2.0
    half = math.radians(180.0 / N_SPOKES)            # half angle between spokes
    # local frame: window bisector along +x
    u1 = V(math.cos(half), math.sin(half), 0)         # axis of spoke above
    n1 = V(math.sin(half), -math.cos(half), 0)        # inward normal, wall 1
    n2 = V(math.sin(half), math.cos(half), 0)         # inward normal, wall 2

    # apex rounding (tangent to both spoke walls, inside the hub)
    ca = V((hw + APEX_R) / math.sin(half), 0, 0)
    ta1 = ca - n1 * APEX_R
    ta2 = ca - n2 * APEX_R
    am = V(ca.x - APEX_R, 0, 0)

    # outer corner rounding (tangent to spoke wall and rim circle)
    s = math.sqrt((OPEN_R - CORNER_R) ** 2 - (hw + CORNER_R) ** 2)
    c1 = n1 * (hw + CORNER_R) + u1 * s
    t1 = n1 * hw + u1 * s                             # tangent point on wall
    t1c = c1 * (OPEN_R / c1.Length)                   # tangent point on rim
    m1 = c1 + ((t1 + t1c) - c1 * 2).normalized() * CORNER_R

    def mir(p):
        return V(p.x, -p.y, 0)

    t2, t2c, m2 = mir(t1), mir(t1c), mir(m1)

    cr = math.cos(math.radians(theta_deg))
    sr = math.sin(math.radians(theta_deg))

    def rot(p):
        return V(p.x * cr - p.y * sr, p.x * sr + p.y * cr, 0)

    a_end = math.degrees(math.atan2(t1c.y, t1c.x))
    edges = [
        cq.Edge.makeLine(rot(ta1), rot(t1)),
        cq.Edge.makeThreePointArc(rot(t1), rot(m1), rot(t1c)),
        # rim arc built as an exact origin-centred circle (same surface as bore)
        cq.Edge.makeCircle(OPEN_R, V(0, 0, 0), V(0, 0, 1),
                           theta_deg - a_end, theta_deg + a_end),
        cq.Edge.makeThreePointArc(rot(t2c), rot(m2), rot(t2)),
        cq.Edge.makeLine(rot(t2), rot(ta2)),
        cq.Edge.makeThreePointArc(rot(ta2), rot(am), rot(ta1)),
    ]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Solid.extrudeLinear(face, V(0, 0, z1 - z0)).translate(V(0, 0, z0))


# ---------------- body ----------------
body = cq.Workplane("XY").circle(R).extrude(H)

# bottom bore leaving a web (spokes) on top
body = body.cut(cq.Workplane("XY").circle(BORE_R).extrude(WEB_Z))

# three windows through the web
for i in range(N_SPOKES):
    spoke_ang = SPOKE0 + i * 360.0 / N_SPOKES
    win_ang = spoke_ang + 180.0 / N_SPOKES
    body = body.cut(cq.Workplane("XY").add(window_solid(win_ang, WEB_Z - 1.0, H + 1.0)))


# round over the top edges of the windows (not the outer rim edge)
def _inner_top_edges(wp):
    out = []
    for e in wp.faces(">Z").edges().vals():
        bb = e.BoundingBox()
        rmax = max(abs(bb.xmin), abs(bb.xmax), abs(bb.ymin), abs(bb.ymax))
        if rmax < R - 1.0:
            out.append(e)
    return out


body = body.newObject(_inner_top_edges(body)).fillet(EDGE_FILLET)

# centre hub, full height
hub = cq.Workplane("XY").circle(HUB_D / 2.0).extrude(H)
result = body.union(hub)
